import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 146.0          # overall length (X)
W = 40.0           # overall width (Y)
T = 10.3           # plate thickness (Z)
R_END = 6.0        # corner radius at the rounded (+X) end
EDGE_R = 0.5       # small round on the outer top / bottom edges

# central window with guide ribs
WIN_X0 = 38.8      # window start (from notch end)
WIN_X1 = 134.0     # window end
WIN_W = 18.4       # window width (Y)
N_RIB = 8          # rib positions (last one merges into the end wall)
RIB_PITCH = 11.87
RIB_X0 = 49.6      # first rib centre
RIB_T = 2.3        # rib thickness (X)
RIB_P = 3.7        # rib protrusion from the long walls (Y)

# holes
HOLE_Y = 13.5      # hole offset from centre line
R_HOLE_X = L - 6.5
R_HOLE_D = 8.5     # through holes at the rounded end
L_HOLE_X = (19.6, 33.1)
L_HOLE_D = 7.8     # blind holes at the notch end
L_HOLE_DEPTH = 8.0
CB_D = 10.0        # counterbore diameter
CB_DEPTH = 1.5
CB_R = 0.6         # round on the counterbore rim

# notch (T-slot) at the -X end
NOTCH_D = 16.3     # notch depth (X)
NOTCH_W = 10.4     # opening width at the top lip
LIP_T = 0.7        # lip thickness
UNDERCUT = 3.6     # undercut below the lip on each side
END_UNDERCUT = 0.8 # undercut below the lip at the notch bottom


def block(x0, x1, y0, y1, z0, z1):
    """Axis aligned box between the given limits."""
    return (
        cq.Workplane("XY")
        .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
        .translate((x0, y0, z0))
    )


# ---------------- base plate ----------------
plate = (
    cq.Workplane("XY")
    .box(L, W, T, centered=(False, True, False))
    .edges("|Z and >X")
    .fillet(R_END)
)
plate = plate.edges("not |Z").fillet(EDGE_R)

# ---------------- window with guide ribs ----------------
win = block(WIN_X0, WIN_X1, -WIN_W / 2.0, WIN_W / 2.0, -1.0, T + 1.0)
for k in range(N_RIB):
    xc = RIB_X0 + k * RIB_PITCH
    x0, x1 = xc - RIB_T / 2.0, xc + RIB_T / 2.0
    if k == N_RIB - 1:          # last rib position merges into the end wall
        x0, x1 = WIN_X1 - RIB_T, WIN_X1 + 1.0
    for s in (1, -1):
        ya = s * WIN_W / 2.0
        yb = s * (WIN_W / 2.0 - RIB_P)
        win = win.cut(block(x0, x1, min(ya, yb) - (1.0 if s < 0 else 0.0),
                            max(ya, yb) + (1.0 if s > 0 else 0.0), -2.0, T + 2.0))
plate = plate.cut(win)

# ---------------- holes ----------------
def hole_tool(d, cb_d, cb_depth, rim_r, z_bottom):
    """Revolved cutter: bore + counterbore with a rounded rim."""
    r, R, f = d / 2.0, cb_d / 2.0, rim_r
    k = 0.70710678
    prof = (
        cq.Workplane("XZ")
        .moveTo(0, T + 1.0)
        .lineTo(R + f, T + 1.0)
        .lineTo(R + f, T)
        .threePointArc((R + f - f * k, T - f + f * k), (R, T - f))
        .lineTo(R, T - cb_depth)
        .lineTo(r, T - cb_depth)
        .lineTo(r, z_bottom)
        .lineTo(0, z_bottom)
        .close()
    )
    return prof.revolve(360, (0, 0, 0), (0, 1, 0))


r_pts = [(R_HOLE_X, HOLE_Y), (R_HOLE_X, -HOLE_Y)]
l_pts = [(x, s * HOLE_Y) for x in L_HOLE_X for s in (1, -1)]
r_tool = hole_tool(R_HOLE_D, CB_D, CB_DEPTH, CB_R, -1.0)
l_tool = hole_tool(L_HOLE_D, CB_D, CB_DEPTH, CB_R, T - L_HOLE_DEPTH)
for (hx, hy) in r_pts:
    plate = plate.cut(r_tool.translate((hx, hy, 0)))
for (hx, hy) in l_pts:
    plate = plate.cut(l_tool.translate((hx, hy, 0)))

# ---------------- notch with undercut lip ----------------
notch_top = block(-1.0, NOTCH_D, -NOTCH_W / 2.0, NOTCH_W / 2.0, -1.0, T + 1.0)
notch_low = block(-1.0, NOTCH_D + END_UNDERCUT,
                  -NOTCH_W / 2.0 - UNDERCUT, NOTCH_W / 2.0 + UNDERCUT,
                  -1.0, T - LIP_T)
plate = plate.cut(notch_top).cut(notch_low)

result = plate

VIEW = {"azimuth": 45, "elevation": 26}
